import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
T = 3.7                     # plate thickness
A_OUT, B_OUT = 50.0, 67.8   # outer ellipse semi-axes (X, Y)
A_IN, B_IN = 35.8, 53.8     # opening ellipse semi-axes (at the bottom face)
# handle side: circular arc through these (half-width, y) points
H_TOP = (13.74, -60.0)
H_MID = (10.7, -100.0)
H_END = (14.56, -145.0)
TIP_Y = -154.7              # chevron tip (90 deg point)
TIP_R = 3.4                 # plan rounding of the point above the lip
TIP_LIP = 1.3               # height of the sharp lip left at the bottom of the point
JUNC_R = 24.0               # plan-view blend radius handle/ring
DRAFT_OUT = 30.0            # draft of the outer side wall (deg)
DRAFT_IN = 30.0             # draft of the opening wall (deg)
R_OUT = 6.0                 # round on top outer edge
R_IN = 5.0                  # round on top inner edge

# underside pockets (centre x, centre y); long side along Y
POCKETS = [(43.6, 3.8), (-43.6, 3.8), (24.0, 51.5), (-24.0, 51.5),
           (12.8, -60.5), (-12.8, -60.5)]
POCKET_L, POCKET_W, POCKET_D = 10.5, 2.6, 1.5
# underside groove along the handle
SLOT_X, SLOT_Y0, SLOT_Y1, SLOT_W, SLOT_D = -8.5, -55.5, -97.0, 2.0, 0.8

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- plan outline (ellipse + handle, tangent blends) ----------------
def circle3(p1, p2, p3):
    (x1, y1), (x2, y2), (x3, y3) = p1, p2, p3
    d = 2 * (x1 * (y2 - y3) + x2 * (y3 - y1) + x3 * (y1 - y2))
    ux = ((x1**2 + y1**2) * (y2 - y3) + (x2**2 + y2**2) * (y3 - y1) + (x3**2 + y3**2) * (y1 - y2)) / d
    uy = ((x1**2 + y1**2) * (x3 - x2) + (x2**2 + y2**2) * (x1 - x3) + (x3**2 + y3**2) * (x2 - x1)) / d
    return (ux, uy), math.hypot(x1 - ux, y1 - uy)


HC, HR = circle3(H_TOP, H_MID, H_END)      # right-hand handle side circle


def _blend(t):
    px, py = A_OUT * math.cos(t), B_OUT * math.sin(t)
    nx, ny = math.cos(t) / A_OUT, math.sin(t) / B_OUT
    n = math.hypot(nx, ny)
    return (px, py), (px + JUNC_R * nx / n, py + JUNC_R * ny / n)


def _gap(t):
    _, (fx, fy) = _blend(t)
    return math.hypot(fx - HC[0], fy - HC[1]) - (HR - JUNC_R)


lo, hi = -math.pi / 2, 0.0
for _ in range(80):
    mid = 0.5 * (lo + hi)
    if _gap(lo) * _gap(mid) <= 0:
        hi = mid
    else:
        lo = mid
T_BLEND = 0.5 * (lo + hi)
P_E, F_C = _blend(T_BLEND)                  # tangent point on ellipse, blend centre
_d = math.hypot(F_C[0] - HC[0], F_C[1] - HC[1])
P_H = (HC[0] + HR * (F_C[0] - HC[0]) / _d, HC[1] + HR * (F_C[1] - HC[1]) / _d)


def _unit(vx, vy):
    n = math.hypot(vx, vy)
    return vx / n, vy / n


_u = _unit((P_E[0] + P_H[0]) / 2 - F_C[0], (P_E[1] + P_H[1]) / 2 - F_C[1])
M_B = (F_C[0] + JUNC_R * _u[0], F_C[1] + JUNC_R * _u[1])        # blend arc midpoint
_a1 = _unit(P_H[0] - HC[0], P_H[1] - HC[1])
_a2 = _unit(H_END[0] - HC[0], H_END[1] - HC[1])
_am = _unit(_a1[0] + _a2[0], _a1[1] + _a2[1])
M_H = (HC[0] + HR * _am[0], HC[1] + HR * _am[1])                # handle arc midpoint


def V(p, s=1.0):
    return cq.Vector(s * p[0], p[1], 0)


END_Y = TIP_Y - 8.0
t_deg = math.degrees(T_BLEND)
edges = [
    cq.Edge.makeEllipse(A_OUT, B_OUT, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), cq.Vector(1, 0, 0),
                        t_deg, 180.0 - t_deg),
    cq.Edge.makeThreePointArc(V(P_E, -1), V(M_B, -1), V(P_H, -1)),
    cq.Edge.makeThreePointArc(V(P_H, -1), V(M_H, -1), V(H_END, -1)),
    cq.Edge.makeLine(V(H_END, -1), cq.Vector(-H_END[0] - 0.6, END_Y, 0)),
    cq.Edge.makeLine(cq.Vector(-H_END[0] - 0.6, END_Y, 0), cq.Vector(H_END[0] + 0.6, END_Y, 0)),
    cq.Edge.makeLine(cq.Vector(H_END[0] + 0.6, END_Y, 0), V(H_END)),
    cq.Edge.makeThreePointArc(V(H_END), V(M_H), V(P_H)),
    cq.Edge.makeThreePointArc(V(P_H), V(M_B), V(P_E)),
]
outline = cq.Wire.assembleEdges(edges)

# ---------------- drafted plate with opening ----------------
body = cq.Solid.extrudeLinear(cq.Face.makeFromWires(outline), cq.Vector(0, 0, T), DRAFT_OUT)
hole_face = cq.Face.makeFromWires(cq.Workplane("XY").ellipse(A_IN, B_IN).val())
hole = cq.Solid.extrudeLinear(hole_face, cq.Vector(0, 0, T), -DRAFT_IN)
body = body.cut(hole)

top = max((f for f in body.Faces() if f.geomType() == "PLANE"), key=lambda f: f.Center().z)
body = body.fillet(R_OUT, top.outerWire().Edges())
top = max((f for f in body.Faces() if f.geomType() == "PLANE"), key=lambda f: f.Center().z)
body = body.fillet(R_IN, [e for w in top.innerWires() for e in w.Edges()])

part = cq.Workplane("XY").add(body)

# ---------------- chevron tip (cut after rounding, shows the section) ----------------
big = 200.0
for s in (1, -1):
    cutter = (
        cq.Workplane("XY")
        .box(big, big, 4 * T, centered=(True, False, True))
        .translate((0, 0, T / 2))
        .rotate((0, 0, 0), (0, 0, 1), 180 + s * 45)
        .translate((0, TIP_Y, 0))
    )
    part = part.cut(cutter)

# upper part of the point is rounded in plan, a sharp lip stays at the bottom
q = TIP_R / math.sqrt(2.0)
tip_relief = (
    cq.Workplane("XY", origin=(0, 0, TIP_LIP))
    .moveTo(q, TIP_Y + q)
    .lineTo(0, TIP_Y - 0.5)
    .lineTo(-q, TIP_Y + q)
    .threePointArc((0, TIP_Y + TIP_R * (math.sqrt(2.0) - 1.0)), (q, TIP_Y + q))
    .close()
    .extrude(2 * T)
)
part = part.cut(tip_relief)

# ---------------- underside pockets and groove ----------------
for (px, py) in POCKETS:
    part = part.cut(cq.Workplane("XY").center(px, py).rect(POCKET_W, POCKET_L).extrude(POCKET_D))

part = part.cut(
    cq.Workplane("XY")
    .center(SLOT_X, (SLOT_Y0 + SLOT_Y1) / 2)
    .rect(SLOT_W, abs(SLOT_Y1 - SLOT_Y0))
    .extrude(SLOT_D)
)

result = part
